import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------------------------------------------------------- parameters (mm)
# gear sector
N_FULL = 17                 # tooth count of the full gear
N_TEETH = 7                 # teeth actually present on the sector
R_TIP = 19.0
R_PITCH = 17.0
R_ROOT = 14.2
R_BODY = 16.55              # plain disc radius outside the toothed sector
MID_TOOTH_ANG = -48.0       # direction of the middle tooth (deg, CCW from +X)
T_GEAR = 12.2               # plate thickness (gear + arm), bottom at Z=0

# hub hole pattern (servo horn style)
HOLE_ANG = -6.3             # direction of the hole line (deg)
HOLE_OFF = 7.6              # side holes distance from centre
D_CENTER = 7.7
D_CB = 11.4                 # counterbore around the side holes (from top)
CB_DEPTH = 3.2
D_SMALL = 4.2

# horn recess in the underside
SLOT_W0 = 12.1              # horn recess width at the hub ...
SLOT_W1 = 11.0              # ... tapering to this width at SLOT_L1 from the centre
SLOT_L1 = 19.0
SLOT_H = 5.0
HUB_R = 7.5
HUB_OFF = (0.7, 0.0)       # hub centre offset (along / across the slot)

# arm / lug
LUG_C = (-9.76, 56.9)       # lug centre (XY)
ARM_W = 9.2
ARM_TILT = 1.6              # arm axis leans this much from +Y (deg)
ARM_END_R = 11.0            # concave end of the arm, concentric with the lug
LUG_R = 9.2
LUG_HOLE = 6.0
LUG_TOP = T_GEAR - 8.4
LUG_T = 9.3

# deep block under the arm
BLOCK_DEPTH = 15.8
BLOCK_Y_LEFT = 25.85        # start of block (-X side)
BLOCK_Y_RIGHT = 30.8        # start of block (+X side)
BLOCK_FACE_SAG = 0.5       # the block's front face is a shallow concave arc

# the finished part sits tipped up slightly about X (lug end higher)
TIP_ANGLE = 0.7

# blend between the arm's outer (-X) side and the gear disc
ARM_BLEND_R = 7.0

# ---------------------------------------------------------------- helpers


def pol(r, a_deg):
    a = math.radians(a_deg)
    return (r * math.cos(a), r * math.sin(a))


pitch = 360.0 / N_FULL
tooth_angs = [MID_TOOTH_ANG + (i - (N_TEETH - 1) / 2.0) * pitch for i in range(N_TEETH)]

# tooth half widths (deg) at flank base / pitch / tip corner (involute-like flank)
HW_BASE = 5.75
HW_PITCH = 4.95
HW_TIP = 2.0
R_FLANK0 = 15.97           # convex flank ends here (base circle) ...
R_FILLET = 14.75           # ... runs radially down to here, then a rounded gap bottom


def toothed_profile():
    """closed outline: centre -> all teeth (with rounded gaps) -> centre"""
    angs = sorted(tooth_angs)
    w = cq.Workplane("XY").moveTo(0, 0)
    w = w.lineTo(*pol(R_FILLET, angs[0] - HW_BASE)).lineTo(*pol(R_FLANK0, angs[0] - HW_BASE))
    for i, a in enumerate(angs):
        w = w.threePointArc(pol(R_PITCH, a - HW_PITCH), pol(R_TIP, a - HW_TIP))
        w = w.threePointArc(pol(R_TIP, a), pol(R_TIP, a + HW_TIP))
        w = w.threePointArc(pol(R_PITCH, a + HW_PITCH), pol(R_FLANK0, a + HW_BASE))
        w = w.lineTo(*pol(R_FILLET, a + HW_BASE))
        if i < len(angs) - 1:
            w = w.threePointArc(pol(R_ROOT, a + pitch / 2.0),
                                pol(R_FILLET, a + pitch - HW_BASE))
            w = w.lineTo(*pol(R_FLANK0, a + pitch - HW_BASE))
    return w.close().extrude(T_GEAR)


# ---------------------------------------------------------------- gear sector
a_first = max(tooth_angs)
a_last = min(tooth_angs)

body = cq.Workplane("XY").circle(R_BODY).extrude(T_GEAR)
# wedge removed where the teeth are
wedge_pts = [(0, 0), pol(40, a_first)]
span = a_first - a_last
for k in range(1, 6):
    wedge_pts.append(pol(40, a_first - span * k / 6.0))
wedge_pts.append(pol(40, a_last))
wedge = cq.Workplane("XY").polyline(wedge_pts).close().extrude(T_GEAR)
body = body.cut(wedge).union(toothed_profile())

# ---------------------------------------------------------------- arm + block + lug
t = math.radians(ARM_TILT)
u = (math.sin(t), math.cos(t))       # arm axis direction (towards lug)
n = (math.cos(t), -math.sin(t))      # arm width direction (+X-ish)


def arm_pt(s, w):
    return (LUG_C[0] + s * u[0] + w * n[0], LUG_C[1] + s * u[1] + w * n[1])


s_start = -LUG_C[1] / u[1]  # reaches Y = 0
arm = (cq.Workplane("XY")
       .polyline([arm_pt(s_start, -ARM_W / 2), arm_pt(s_start, ARM_W / 2),
                  arm_pt(0, ARM_W / 2), arm_pt(0, -ARM_W / 2)]).close()
       .extrude(T_GEAR))


def s_at_y(y, w):
    # parameter s along axis where the edge at offset w reaches Y=y
    return (y - LUG_C[1] - w * n[1]) / u[1]


bl = arm_pt(s_at_y(BLOCK_Y_LEFT, -ARM_W / 2), -ARM_W / 2)
br = arm_pt(s_at_y(BLOCK_Y_RIGHT, ARM_W / 2), ARM_W / 2)
# mid point of the concave front face
_cx, _cy = (bl[0] + br[0]) / 2.0, (bl[1] + br[1]) / 2.0
_dx, _dy = br[0] - bl[0], br[1] - bl[1]
_L = math.hypot(_dx, _dy)
bm = (_cx - BLOCK_FACE_SAG * _dy / _L, _cy + BLOCK_FACE_SAG * _dx / _L)
block = (cq.Workplane("XY").workplane(offset=-BLOCK_DEPTH)
         .moveTo(*bl).threePointArc(bm, br)
         .lineTo(*arm_pt(0, ARM_W / 2)).lineTo(*arm_pt(0, -ARM_W / 2)).close()
         .extrude(BLOCK_DEPTH + 0.01))

end_cut = (cq.Workplane("XY").workplane(offset=-BLOCK_DEPTH - 1)
           .center(*LUG_C).circle(ARM_END_R).extrude(T_GEAR + BLOCK_DEPTH + 2))
arm = arm.union(block).cut(end_cut)

neck = (cq.Workplane("XY").workplane(offset=LUG_TOP - LUG_T)
        .polyline([arm_pt(-ARM_END_R - 0.5, -ARM_W / 2), arm_pt(-ARM_END_R - 0.5, ARM_W / 2),
                   arm_pt(0, ARM_W / 2), arm_pt(0, -ARM_W / 2)]).close()
        .extrude(LUG_T))
lug = (cq.Workplane("XY").workplane(offset=LUG_TOP - LUG_T)
       .center(*LUG_C).circle(LUG_R).extrude(LUG_T))
lug = lug.union(neck)
lug = lug.cut(cq.Workplane("XY").workplane(offset=LUG_TOP - LUG_T - 1)
              .center(*LUG_C).circle(LUG_HOLE / 2).extrude(LUG_T + 2))

part = body.union(arm)

# the arm's -X side runs into the gear disc with a soft blend: find that junction line
_px, _py = LUG_C[0] - ARM_W / 2 * n[0], LUG_C[1] - ARM_W / 2 * n[1]
_b = _px * u[0] + _py * u[1]
_c = _px * _px + _py * _py - R_BODY * R_BODY
_s = -_b - math.sqrt(_b * _b - _c)          # first hit coming from the gear side
_s = max(_s, -_b + math.sqrt(_b * _b - _c)) if (_py + _s * u[1]) < 0 else _s
jx, jy = _px + _s * u[0], _py + _s * u[1]
part = (part.edges(cq.selectors.NearestToPointSelector((jx, jy, T_GEAR / 2.0)))
        .fillet(ARM_BLEND_R))
part = part.union(lug)

# ---------------------------------------------------------------- hub holes
ha = math.radians(HOLE_ANG)
hd = (math.cos(ha), math.sin(ha))
side = [(HOLE_OFF * hd[0], HOLE_OFF * hd[1]), (-HOLE_OFF * hd[0], -HOLE_OFF * hd[1])]

cbs = (cq.Workplane("XY").workplane(offset=T_GEAR - CB_DEPTH)
       .pushPoints(side).circle(D_CB / 2).extrude(CB_DEPTH + 1))
part = part.cut(cbs)
thru = (cq.Workplane("XY").workplane(offset=-1)
        .pushPoints(side).circle(D_SMALL / 2).extrude(T_GEAR + 2))
part = part.cut(thru)
part = part.cut(cq.Workplane("XY").workplane(offset=-1).circle(D_CENTER / 2).extrude(T_GEAR + 2))

# ---------------------------------------------------------------- horn recess underneath
_L = 36.0
_wL = SLOT_W0 / 2 - (SLOT_W0 - SLOT_W1) / 2 * _L / SLOT_L1
slot = (cq.Workplane("XY").workplane(offset=-1)
        .transformed(rotate=(0, 0, HOLE_ANG))
        .polyline([(-_L, -_wL), (0, -SLOT_W0 / 2), (_L, -_wL),
                   (_L, _wL), (0, SLOT_W0 / 2), (-_L, _wL)]).close()
        .extrude(SLOT_H + 1))
_hx = HUB_OFF[0] * hd[0] - HUB_OFF[1] * hd[1]
_hy = HUB_OFF[0] * hd[1] + HUB_OFF[1] * hd[0]
hub = (cq.Workplane("XY").workplane(offset=-1).center(_hx, _hy)
       .circle(HUB_R).extrude(SLOT_H + 1))
part = part.cut(slot.union(hub))

result = part.rotate((0, 0, 0), (1, 0, 0), TIP_ANGLE)
